import math
import cadquery as cq

# Four-legged stand: a flat ring (with a split cross bar in its opening) carried
# by four flat-topped arms that bend smoothly down into round legs.
#
# ---------------- driving dimensions (mm) ----------------
H = 172.0          # overall height (floor to top face)
LEG_X = 46.0       # leg centre offset along X
LEG_Y = 110.0      # leg centre offset along Y
LEG_D = 18.0       # leg diameter
ARM_T = 6.8        # arm thickness below the top face
SEC_H = 14.0       # height of the swept obround section (its top is cut off)
BEND_R = 16.0      # centre-line bend radius leg -> arm
ARM_START = 42.0   # radial distance at which the arms start (inside ring)
RING_OD = 110.0    # ring outer diameter
RING_ID = 74.0     # ring inner diameter
RING_T = 7.2       # ring thickness
BAR_W = 15.0       # width of the bar crossing the ring opening (along Y)
HOLE_R = 2.5       # corner radius of the two D openings
NOTCH_D = 5.7      # depth of each notch cut in the bar sides
NOTCH_H = 4.7      # notch height (along Y)
NOTCH_R = 1.0      # notch inner corner radius
NOTCH_EDGE_R = 0.8 # notch entrance corner radius
SLIT = 0.2         # thin slit splitting the bar neck
ROD_GAP = 0.05     # section kept a hair inside the leg (robust booleans)
CAP_INSET = 0.1    # top cap over the bend, a hair smaller than the section

VIEW = {"azimuth": 45, "elevation": 26}

z_top = H
r_leg = LEG_D / 2.0

# ---------------- ring with cross bar ----------------
# (cylinder seams are turned to places where they stay hidden)
ARM_DIR = math.degrees(math.atan2(LEG_Y, LEG_X))
ring_solid = cq.Solid.makeCylinder(
    RING_OD / 2.0, RING_T, cq.Vector(0, 0, z_top - RING_T), cq.Vector(0, 0, 1)
).rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), ARM_DIR)
ring = cq.Workplane("XY").add(ring_solid)

ri = RING_ID / 2.0
zc0 = z_top - RING_T - 1.0
for sgn in (-1, 1):
    # D opening = hole circle intersected with the half plane beyond the bar
    disc = cq.Workplane("XY").add(
        cq.Solid.makeCylinder(ri, RING_T + 2, cq.Vector(0, 0, zc0), cq.Vector(0, 0, 1))
        .rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), 90)
    )
    half = (
        cq.Workplane("XY")
        .workplane(offset=zc0)
        .center(sgn * (BAR_W / 2.0 + ri), 0)
        .rect(2 * ri, 2 * ri + 2)
        .extrude(RING_T + 2)
    )
    d_cut = disc.intersect(half).edges("|Z").fillet(HOLE_R)
    ring = ring.cut(d_cut)

# notches either side of the bar centre + thin slit through the neck
for sgn in (-1, 1):
    notch = (
        cq.Workplane("XY")
        .workplane(offset=zc0)
        .center(sgn * (BAR_W / 2.0 - NOTCH_D + (NOTCH_D + 3.0) / 2.0), 0)
        .rect(NOTCH_D + 3.0, NOTCH_H)
        .extrude(RING_T + 2)
    )
    notch = notch.edges("|Z").fillet(NOTCH_R)
    ring = ring.cut(notch)
slit = (
    cq.Workplane("XY")
    .workplane(offset=zc0)
    .rect(BAR_W, SLIT)
    .extrude(RING_T + 2)
)
ring = ring.cut(slit)

# soften the convex corners at the notch entrances
def _notch_entry(e):
    p = e.positionAt(0.5)
    return (
        abs(abs(p.x) - BAR_W / 2.0) < 1e-3
        and abs(abs(p.y) - NOTCH_H / 2.0) < 1e-3
        and abs(e.positionAt(0).z - e.positionAt(1).z) > 1.0
    )

ring = cq.Workplane("XY").add(
    ring.val().fillet(NOTCH_EDGE_R, [e for e in ring.val().Edges() if _notch_entry(e)])
)


# ---------------- legs + arms ----------------
def leg_arm(px, py):
    """Straight leg plus a bent bar (obround section) running from
    inside the leg into the arm; the top is later flattened at z = H."""
    L = math.hypot(px, py)
    ux, uy = -px / L, -py / L              # unit vector leg -> centre
    za = z_top - ARM_T + SEC_H / 2.0       # axis height of the arm section

    def P(q, z):
        return cq.Vector(px + q * ux, py + q * uy, z)

    c45 = math.cos(math.radians(45))
    # centre line: short vertical run inside the leg, quarter bend, arm
    a = P(0, za - BEND_R - 2.0)
    b = P(0, za - BEND_R)
    m = P(BEND_R * (1 - c45), za - BEND_R * (1 - c45))
    d = P(BEND_R, za)
    e = P(L - ARM_START, za)
    path = cq.Wire.assembleEdges(
        [
            cq.Edge.makeLine(a, b),
            cq.Edge.makeThreePointArc(b, m, d),
            cq.Edge.makeLine(d, e),
        ]
    )
    # swept section: obround as wide as the leg (a hair less) so that it
    # stays inside the leg where the path runs down the leg axis
    lat = cq.Vector(-uy, ux, 0)
    sec_plane = cq.Plane(origin=a, xDir=lat, normal=cq.Vector(0, 0, 1))
    prof = cq.Workplane(sec_plane).slot2D(2 * (r_leg - ROD_GAP), SEC_H).val()
    rod = cq.Solid.sweep(prof, [], path, makeSolid=True, isFrenet=False)
    # straight cap over the bend keeps the top face full width up to the leg
    cap_plane = cq.Plane(origin=P(0, za), xDir=lat, normal=cq.Vector(ux, uy, 0))
    cap = (
        cq.Workplane(cap_plane)
        .slot2D(2 * (r_leg - ROD_GAP) - CAP_INSET, SEC_H - CAP_INSET)
        .extrude(BEND_R + 2.0)
        .val()
    )

    # straight leg, seam turned to -X where it is least visible
    leg = cq.Solid.makeCylinder(r_leg, z_top, cq.Vector(0, 0, 0), cq.Vector(0, 0, 1))
    leg = leg.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), 180).translate(
        cq.Vector(px, py, 0)
    )
    return (
        cq.Workplane("XY")
        .add(leg)
        .union(cq.Workplane("XY").add(rod))
        .union(cq.Workplane("XY").add(cap))
    )


body = ring
for sx in (-1, 1):
    for sy in (-1, 1):
        body = body.union(leg_arm(sx * LEG_X, sy * LEG_Y))

# flatten everything at the top plane (arms, leg tops and ring share it)
top_cut = (
    cq.Workplane("XY")
    .box(1000, 1000, 100, centered=(True, True, False))
    .translate((0, 0, z_top))
)
result = body.cut(top_cut)
